import cadquery as cq

# ---------------------------------------------------------------------------
# Adapter plate with central window, counterbored corner holes, clearance
# holes and four standoff bosses.  Origin = centre of the main square /
# window, Z = 0 on the underside of the plate.
# ---------------------------------------------------------------------------

T = 7.5                 # plate thickness

# main rounded square
SQ_W = 102.2            # X size
SQ_H = 102.4            # Y size
SQ_R = 5.6              # corner radius (meets the band end tangentially)

# side band (slightly wider than the square, shorter in Y)
BAND_HALF_Y = 45.5
BAND_XR = 54.3          # right band edge
BAND_XL_TOP = -59.4     # left band edge (upper ear)
BAND_XL_BOT = -58.6     # left band edge (lower ear)
BAND_BOT_CH = 2.4       # chamfer at lower-left band corner
EAR_R_RIGHT = 0.6       # rounding of the right band corners
EAR_R_LEFT = 0.9        # rounding of the upper-left band corner

# left tab carrying the two left bosses
TAB_XL = -64.1
TAB_Y_TOP = 40.8        # where the upper 45deg chamfer starts on the band edge
TAB_Y_BOT = -24.3       # where the lower 45deg chamfer starts on the band edge

# central window
WIN_W = 56.4
WIN_H = 69.8
WIN_R = 5.2

# counterbored corner holes
CB_POS = 42.75
CB_D = 9.25
CB_DEPTH = 3.5
CB_THRU = 6.4

# plain clearance holes
BIG_X = 39.75
BIG_Y = 25.7
BIG_D = 10.8

# standoff bosses
BOSS_D = 8.5
BOSS_H = 8.75           # height above plate top
BOSS_HOLE = 4.7
BOSS_FILLET = 2.8
BOSSES = [(-59.1, 32.65), (-59.1, -15.15), (30.4, 41.4), (28.4, -41.65)]

# angular position of cylinder seams (purely cosmetic)
SEAM_OUT = 135.0        # bosses
SEAM_IN = 45.0          # holes (seam lies on the silhouette in the iso views)


# ---------------------------------------------------------------------------
class NearXY(cq.Selector):
    """Select objects whose centre lies near one of the given XY points."""

    def __init__(self, pts, tol=0.3):
        self.pts = pts
        self.tol = tol

    def filter(self, objs):
        out = []
        for o in objs:
            c = o.Center()
            for (x, y) in self.pts:
                if abs(c.x - x) < self.tol and abs(c.y - y) < self.tol:
                    out.append(o)
                    break
        return out


def outline_solid(height):
    """Plate outline extruded from z=0 to `height`."""
    sq = (cq.Workplane("XY")
          .rect(SQ_W, SQ_H).extrude(height)
          .edges("|Z").fillet(SQ_R))

    x_in = SQ_W / 2 - SQ_R - 1.0
    right = (cq.Workplane("XY")
             .center((x_in + BAND_XR) / 2, 0)
             .rect(BAND_XR - x_in, 2 * BAND_HALF_Y)
             .extrude(height)
             .edges("|Z").edges(">X").fillet(EAR_R_RIGHT))

    left_pts = [
        (-x_in, BAND_HALF_Y),
        (BAND_XL_TOP, BAND_HALF_Y),
        (BAND_XL_TOP, TAB_Y_TOP),
        (TAB_XL, TAB_Y_TOP - (BAND_XL_TOP - TAB_XL)),
        (TAB_XL, TAB_Y_BOT + (BAND_XL_BOT - TAB_XL)),
        (BAND_XL_BOT, TAB_Y_BOT),
        (BAND_XL_BOT, -BAND_HALF_Y + BAND_BOT_CH),
        (BAND_XL_BOT + BAND_BOT_CH, -BAND_HALF_Y),
        (-x_in, -BAND_HALF_Y),
    ]
    left = cq.Workplane("XY").polyline(left_pts).close().extrude(height)
    left = left.edges("|Z").edges(NearXY([(BAND_XL_TOP, BAND_HALF_Y)])).fillet(EAR_R_LEFT)

    return sq.union(right).union(left).clean()


def cylinder(x, y, z0, d, h, seam_deg):
    """Vertical cylinder with its seam placed at a chosen angle."""
    c = cq.Solid.makeCylinder(d / 2, h, cq.Vector(0, 0, z0), cq.Vector(0, 0, 1))
    c = c.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), seam_deg)
    return c.translate(cq.Vector(x, y, 0))


plate = outline_solid(T)

# central window
window = (cq.Workplane("XY").workplane(offset=-1)
          .rect(WIN_W, WIN_H).extrude(T + 2)
          .edges("|Z").fillet(WIN_R))
plate = plate.cut(window)

# plain clearance holes
for sx in (-1, 1):
    for sy in (-1, 1):
        plate = plate.cut(cylinder(sx * BIG_X, sy * BIG_Y, -1, BIG_D, T + 2, SEAM_IN))

# counterbored corner holes
for sx in (-1, 1):
    for sy in (-1, 1):
        x, y = sx * CB_POS, sy * CB_POS
        plate = plate.cut(cylinder(x, y, -1, CB_THRU, T + 2, SEAM_IN))
        plate = plate.cut(cylinder(x, y, T - CB_DEPTH, CB_D, CB_DEPTH + 1, SEAM_IN))

# standoff bosses with a filleted foot (revolved profile), trimmed to outline
r = BOSS_D / 2
f = BOSS_FILLET
k = 0.70710678
boss_profile = (cq.Workplane("XZ")
                .moveTo(0, T)
                .lineTo(r + f, T)
                .threePointArc((r + f - f * k, T + f - f * k), (r, T + f))
                .lineTo(r, T + BOSS_H)
                .lineTo(0, T + BOSS_H)
                .close()
                .revolve(360, (0, 0, 0), (0, 1, 0))
                .val()
                .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), SEAM_OUT))

clip = outline_solid(T + BOSS_H + 1).val()
for (bx, by) in BOSSES:
    b = boss_profile
    if bx < 0:
        # edge bosses: put the seam where the foot fillet gets trimmed away
        b = b.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 180.0 - SEAM_OUT)
    b = b.translate(cq.Vector(bx, by, 0)).intersect(clip)
    plate = plate.union(b)

# through holes of the bosses
for (bx, by) in BOSSES:
    plate = plate.cut(cylinder(bx, by, -1, BOSS_HOLE, T + BOSS_H + 2, SEAM_IN))

result = plate.clean()
